import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------
W = 61.2          # width (X) of block and plate
LP = 100.0        # plate length (Y)
LB = 82.8         # block length (Y)
HB = 24.4         # block height (Z)
TP = 3.2          # plate thickness

# bottom groove (open to the front face)
G_W = 11.6        # groove width
G_H = 4.4         # groove height
G_R = 2.6         # fillet radius of groove roof
G_LEN = 22.0      # groove length from the front face (to tip of round end)

# small rectangular pocket in the front face, directly under the plate
FP_X = 16.1       # centre X
FP_W = 7.4        # width
FP_H = 5.5        # height (down from block top)
FP_D = 2.6        # depth into the block
FP_CH_W = 2.0     # small channel leaving the pocket at its top-left corner
FP_CH_H = 1.1
FP_CH_D = 3.0

# countersunk holes in the bottom face
BH_D = 3.0
BH_CSK = 8.0
BH_DEPTH = 12.0
BH_POS = [(-14.5, 23.4), (14.5, 23.4), (-23.2, 75.0), (23.2, 75.0)]

# small rectangular pocket in the bottom face
RP_X, RP_Y = -21.4, 37.3
RP_LX, RP_LY, RP_D = 10.8, 8.25, 3.6

# plate features
PIN_Y = 12.6
PIN_HOLE_D = 12.6
SLOT_X = 6.5
SLOT_Y = 44.3
SLOT_W = 5.0
SLOT_L = 7.0
BIG_Y = 88.0
BIG_D = 9.0
SMALL_Y = 93.6
SMALL_D = 5.0
CB_DEPTH = 1.5        # counterbore depth on the underside of the plate holes
CB_EXTRA = 2.4        # counterbore oversize (diameter) for the slots
REC_W = 24.0          # underside recess around the back holes (X width)
REC_Y0 = 83.3         # recess start (Y)
REC_Y1 = 97.8         # recess end (Y)

# pin
HEAD_D = 13.7
HEAD_FLATS = 12.4
HEAD_H = 8.5
SHANK_D = 11.3        # shank diameter
SHANK_ABOVE = 6.6     # shank height above plate top
SLIT_W = 0.6          # width of the radial axial slits in the shank
SLIT_R0 = 1.5         # slits run from this radius outwards
SLIT_ANGLES = (-75.0, -25.0, 120.0, 150.0)

# ---------------------------------------------------------------
# Block
# ---------------------------------------------------------------
block = cq.Workplane("XY").box(W, LB, HB, centered=(True, False, False))

# groove cutter: stadium in plan, filleted roof
g_start = -8.0
g_total = G_LEN - g_start
groove = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .center(0, g_start + g_total / 2.0)
    .slot2D(g_total, G_W, 90)
    .extrude(G_H + 1.0)
    .faces(">Z")
    .edges()
    .fillet(G_R)
)
block = block.cut(groove)

# front pocket (rectangular, open to the front face and to the block top)
fp = cq.Workplane("XY").box(FP_W, FP_D + 1.0, FP_H + 1.0, centered=(True, False, False)) \
    .translate((FP_X, -1.0, HB - FP_H))
block = block.cut(fp)
fp_ch = cq.Workplane("XY").box(FP_CH_W, FP_CH_D + 0.5, FP_CH_H + 1.0, centered=(False, False, False)) \
    .translate((FP_X - FP_W / 2.0, FP_D - 0.5, HB - FP_CH_H))
block = block.cut(fp_ch)

# countersunk bottom holes
for (x, y) in BH_POS:
    cyl = cq.Solid.makeCylinder(BH_D / 2.0, BH_DEPTH + 1.0,
                                cq.Vector(x, y, -1.0), cq.Vector(0, 0, 1))
    h_csk = (BH_CSK - BH_D) / 2.0
    cone = cq.Solid.makeCone(BH_CSK / 2.0 + 1.0, BH_D / 2.0, h_csk + 1.0,
                             cq.Vector(x, y, -1.0), cq.Vector(0, 0, 1))
    block = block.cut(cq.Workplane("XY").add(cyl)).cut(cq.Workplane("XY").add(cone))

# rectangular bottom pocket
rp = cq.Workplane("XY").box(RP_LX, RP_LY, RP_D + 1.0, centered=(True, True, False)) \
    .translate((RP_X, RP_Y, -1.0))
block = block.cut(rp)

# ---------------------------------------------------------------
# Top plate
# ---------------------------------------------------------------
plate = (
    cq.Workplane("XY")
    .workplane(offset=HB)
    .center(0, LP / 2.0)
    .rect(W, LP)
    .extrude(TP)
)
cut_wp = cq.Workplane("XY").workplane(offset=HB - 1.0)
plate = plate.cut(cut_wp.center(0, PIN_Y).circle(PIN_HOLE_D / 2.0).extrude(TP + 2))
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=HB - 1.0)
    .pushPoints([(-SLOT_X, SLOT_Y), (SLOT_X, SLOT_Y)])
    .slot2D(SLOT_L, SLOT_W, 90)
    .extrude(TP + 2)
)
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=HB - 1.0)
    .center(0, BIG_Y).circle(BIG_D / 2.0).extrude(TP + 2)
)
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=HB - 1.0)
    .pushPoints([(-SLOT_X, SMALL_Y), (SLOT_X, SMALL_Y)])
    .circle(SMALL_D / 2.0)
    .extrude(TP + 2)
)
# counterbores from the underside of the plate
cb_wp = lambda: cq.Workplane("XY").workplane(offset=HB - 1.0)
plate = plate.cut(
    cb_wp().pushPoints([(-SLOT_X, SLOT_Y), (SLOT_X, SLOT_Y)])
    .slot2D(SLOT_L + CB_EXTRA, SLOT_W + CB_EXTRA, 90)
    .extrude(CB_DEPTH + 1.0)
)
# shallow recess on the underside of the overhang around the three back holes
plate = plate.cut(
    cb_wp().center(0, (REC_Y0 + REC_Y1) / 2.0)
    .rect(REC_W, REC_Y1 - REC_Y0)
    .extrude(CB_DEPTH + 1.0)
)

# ---------------------------------------------------------------
# Pin (slotted round shank + round head with two flats)
# ---------------------------------------------------------------
shank_h = TP + SHANK_ABOVE
shank = (
    cq.Workplane("XY")
    .workplane(offset=HB)
    .center(0, PIN_Y)
    .circle(SHANK_D / 2.0)
    .extrude(shank_h)
)
for ang in SLIT_ANGLES:
    slit = (
        cq.Workplane("XY")
        .box(SHANK_D / 2.0 + 1.0 - SLIT_R0, SLIT_W, shank_h, centered=(False, True, False))
        .translate((SLIT_R0, 0, 0))
        .rotate((0, 0, 0), (0, 0, 1), ang)
        .translate((0, PIN_Y, HB))
    )
    shank = shank.cut(slit)
head_z = HB + shank_h
head = (
    cq.Workplane("XY")
    .workplane(offset=head_z)
    .center(0, PIN_Y)
    .circle(HEAD_D / 2.0)
    .extrude(HEAD_H)
)
head = head.intersect(
    cq.Workplane("XY").box(HEAD_FLATS, HEAD_D + 2, HEAD_H, centered=(True, True, False))
    .translate((0, PIN_Y, head_z))
)
pin = shank.union(head)

result = (
    cq.Workplane("XY")
    .newObject([cq.Compound.makeCompound([
        block.val(), plate.val(), pin.val()
    ])])
)

VIEW = {"azimuth": 45, "elevation": 26}
